import cadquery as cq

# Driving dimensions (mm)
R_FLANGE = 30.0        # radius of the rounded (D) end of the flange
FLAT_OFFSET = 23.0     # distance from boss axis to the flat end of the flange
T_FLANGE = 8.0         # flange thickness
R_BOSS = 19.5          # boss (cylinder) radius
H_TOTAL = 40.0         # overall height (flange + boss)
R_TOP_FILLET = 5.0     # fillet around the top edge of the boss
SEAM_ANGLE = 135.0     # where the boss's cylindrical seam sits (purely cosmetic: back side)

# D-shaped flange: flat end at -X, semicircular end at +X centred on the boss axis
flange = (
    cq.Workplane("XY")
    .moveTo(-FLAT_OFFSET, -R_FLANGE)
    .lineTo(0, -R_FLANGE)
    .threePointArc((R_FLANGE, 0), (0, R_FLANGE))
    .lineTo(-FLAT_OFFSET, R_FLANGE)
    .close()
    .extrude(T_FLANGE)
)

# Cylindrical boss standing on the flange, rounded top edge
boss = (
    cq.Workplane("XY")
    .workplane(offset=T_FLANGE)
    .circle(R_BOSS)
    .extrude(H_TOTAL - T_FLANGE)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    .faces(">Z").edges()
    .fillet(R_TOP_FILLET)
)

result = flange.union(boss)

VIEW = {"azimuth": 45, "elevation": 26}
